import cadquery as cq

# Cylindrical spacer / standoff with a plain through bore.
# Top outside and top bore edges are rounded, bottom edges are sharp.

# Driving dimensions (mm)
OUTER_D = 20.0           # outside diameter of the spacer
INNER_D = 10.0           # through-bore diameter
HEIGHT = 23.8            # overall length (axis along +Z)
TOP_OUTER_FILLET = 0.75  # round on top outside edge
TOP_INNER_FILLET = 0.75  # round on top bore edge

ro = OUTER_D / 2.0
ri = INNER_D / 2.0

# Tube body: annulus extruded along +Z
body = (
    cq.Workplane("XY")
    .circle(ro)
    .circle(ri)
    .extrude(HEIGHT)
)

# Edge treatment on the top end only
body = body.faces(">Z").edges(cq.selectors.RadiusNthSelector(1)).fillet(TOP_OUTER_FILLET)
body = body.faces(">Z").edges(cq.selectors.RadiusNthSelector(0)).fillet(TOP_INNER_FILLET)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
